import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 150.0            # overall length along X
T = 4.8              # base plate thickness
Y_BACK = 11.3        # back edge of end regions (rod axis at Y=0)
Y_FRONT = -11.3      # front edge of bar
Y_NARROW = 4.6       # back edge of narrow middle section
# end widening (diagonals)
XL_D0, XL_D1 = 17.6, 28.2     # left diagonal  (x at back, x at narrow)
XR_D0, XR_D1 = 116.7, 125.2   # right diagonal (x at narrow, x at back)

# flange
FX0, FX1 = 31.0, 110.0
FY = -29.2           # flange front edge
ARC_CX, ARC_CY, ARC_R = 59.2, -61.2, 39.4   # concave arc on flange front
F_HOLE_D = 4.5
F_HOLES = [(37.3, -22.6), (104.1, -22.6)]
F_CORNER_L, F_CORNER_R = 5.0, 5.0
# flange pocket
FP_D = 1.4
FP_Y_TOP = -15.0
FP_X0, FP_X1 = 41.0, 104.6
FP_Y_STEP = -17.1
FP_Y_BOT = -23.8
FP_BOSS_C = (103.6, -23.8)
FP_BOSS_R = 6.7
FP_ARC_R = ARC_R + 3.8

# lug (left end)
LUG_T = 6.5
LUG_R = 11.3
AXIS_Z = 20.1        # rod axis height
LUG_HOLE_D = 14.2

# clamp block (right end)
BLK_X = 11.4
BLK_H = 27.4
SLOT_W = 10.4
SLOT_R = 7.8
SLOT_UNDERCUT_Z = AXIS_Z - 5.1
TAP_D = 3.6          # threaded hole in front prong
CLR_D = 4.6          # clearance hole in back prong
CB_D, CB_DEPTH = 7.6, 2.5   # counterbore on back face
CROSS_Z = 19.2
BLK_TOP_FILLET = 1.6
BLK_EDGE_FILLET = 0.8

# rails
RAIL_H = 3.6
RAIL_FOOT_R = 0.6
FR_X0, FR_X1 = 10.2, 134.2
FR_Y0, FR_Y1 = -10.4, -7.4
BR_X0, BR_X1 = XL_D1, XR_D0
BR_Y0, BR_Y1 = 0.1, 3.5

# recesses
SLOT_D = 1.7
SLOT_X0, SLOT_X1 = 27.1, 117.8
SLOT_Y0, SLOT_Y1 = -6.8, -0.6
BRIDGE_X0, BRIDGE_X1 = 70.5, 74.3
EP_D = 2.4
EP_Y0, EP_Y1 = -6.8, 7.0
EPL_X0, EPL_X1 = 10.0, 22.9
EPR_X0, EPR_X1 = 122.1, 134.2
EP_CHX, EP_CHY = 6.0, 4.4    # chamfer on end pocket corner

# ---------------- base plate ----------------
bar_pts = [
    (0.0, Y_FRONT), (L, Y_FRONT), (L, Y_BACK), (XR_D1, Y_BACK),
    (XR_D0, Y_NARROW), (XL_D1, Y_NARROW), (XL_D0, Y_BACK), (0.0, Y_BACK),
]
base = cq.Workplane("XY").polyline(bar_pts).close().extrude(T)
base = base.edges("|Z and >X").fillet(BLK_EDGE_FILLET)

# flange: rectangle minus concave arc, with rounded front corners
flange = (
    cq.Workplane("XY")
    .center((FX0 + FX1) / 2, (Y_FRONT + 1.0 + FY) / 2)
    .rect(FX1 - FX0, (Y_FRONT + 1.0) - FY)
    .extrude(T)
)
flange = flange.edges("|Z and <Y and <X").fillet(F_CORNER_L)
flange = flange.edges("|Z and <Y and >X").fillet(F_CORNER_R)
arc_cut = cq.Workplane("XY").center(ARC_CX, ARC_CY).circle(ARC_R).extrude(T)
flange = flange.cut(arc_cut)
base = base.union(flange)

# ---------------- lug ----------------
lug = (
    cq.Workplane("YZ")
    .moveTo(Y_FRONT, 0)
    .lineTo(Y_BACK, 0)
    .lineTo(Y_BACK, AXIS_Z)
    .threePointArc((0, AXIS_Z + LUG_R), (Y_FRONT, AXIS_Z))
    .close()
    .extrude(LUG_T)
)
lug_hole = (
    cq.Workplane("YZ").center(0, AXIS_Z).circle(LUG_HOLE_D / 2).extrude(LUG_T)
)
lug = lug.cut(lug_hole)

# ---------------- clamp block ----------------
BX0 = L - BLK_X
blk = (
    cq.Workplane("XY")
    .box(BLK_X, Y_BACK - Y_FRONT, BLK_H, centered=False)
    .translate((BX0, Y_FRONT, 0))
)
blk = blk.edges("|Z and >X").fillet(BLK_EDGE_FILLET)
# slot with cylindrical bottom (slight undercut, as printed)
slot_bottom = AXIS_Z - math.sqrt(SLOT_R ** 2 - (SLOT_W / 2) ** 2)
slot = (
    cq.Workplane("YZ")
    .center(0, (slot_bottom + BLK_H + 2) / 2)
    .rect(SLOT_W, BLK_H + 2 - slot_bottom)
    .extrude(BLK_X + 2)
    .translate((BX0 - 1, 0, 0))
)
bore = (
    cq.Workplane("YZ").center(0, AXIS_Z).circle(SLOT_R).extrude(BLK_X + 2)
    .translate((BX0 - 1, 0, 0))
)
bore_lim = (
    cq.Workplane("XY")
    .box(BLK_X + 2, 2 * SLOT_R + 2, SLOT_UNDERCUT_Z, centered=(True, True, False))
    .translate((L - BLK_X / 2, 0, 0))
)
blk = blk.cut(slot).cut(bore.intersect(bore_lim))
blk = blk.faces(">Z").edges().fillet(BLK_TOP_FILLET)

# cross screw: tapped in front prong, clearance + counterbore in back prong
XC = L - BLK_X / 2
tap = (
    cq.Workplane("XZ").center(XC, CROSS_Z).circle(TAP_D / 2)
    .extrude(-12.0).translate((0, Y_FRONT - 1, 0))
)
clr = (
    cq.Workplane("XZ").center(XC, CROSS_Z).circle(CLR_D / 2)
    .extrude(-10.0).translate((0, 2.0, 0))
)
cbore = (
    cq.Workplane("XZ").center(XC, CROSS_Z).circle(CB_D / 2)
    .extrude(-(CB_DEPTH + 1)).translate((0, Y_BACK - CB_DEPTH, 0))
)
blk = blk.cut(tap).cut(clr).cut(cbore)

# ---------------- rails ----------------
def rail(x0, x1, y0, y1):
    """Rib with rounded (stadium) ends and a rounded top."""
    w = y1 - y0
    r = (
        cq.Workplane("XY").workplane(offset=T)
        .center((x0 + x1) / 2, (y0 + y1) / 2)
        .slot2D(x1 - x0, w)
        .extrude(RAIL_H)
    )
    r = r.faces(">Z").edges().fillet(w * 0.47)
    return r

rails = rail(FR_X0, FR_X1, FR_Y0, FR_Y1).union(rail(BR_X0, BR_X1, BR_Y0, BR_Y1))

part = base.union(lug).union(blk).union(rails)

# small concave fillet where the ribs meet the plate
def rail_foot_edges(x0, x1, y0, y1):
    return cq.selectors.BoxSelector((x0 - 0.3, y0 - 0.3, T - 0.01), (x1 + 0.3, y1 + 0.3, T + 0.01))

part = part.edges(rail_foot_edges(FR_X0, FR_X1, FR_Y0, FR_Y1)).fillet(RAIL_FOOT_R)
part = part.edges(rail_foot_edges(BR_X0, BR_X1, BR_Y0, BR_Y1)).fillet(RAIL_FOOT_R * 0.7)

# ---------------- recesses ----------------
def box_cut(x0, x1, y0, y1, d):
    return (
        cq.Workplane("XY").box(x1 - x0, y1 - y0, d + 1, centered=False)
        .translate((x0, y0, T - d))
    )

# long channel between rails, split by a bridge
part = part.cut(box_cut(SLOT_X0, BRIDGE_X0, SLOT_Y0, SLOT_Y1, SLOT_D))
part = part.cut(box_cut(BRIDGE_X1, SLOT_X1, SLOT_Y0, SLOT_Y1, SLOT_D))

# end pockets (rectangles with one chamfered corner following the outline)
def end_pocket(x0, x1, left):
    if left:
        pts = [(x0, EP_Y0), (x1, EP_Y0), (x1, EP_Y1 - EP_CHY),
               (x1 - EP_CHX, EP_Y1), (x0, EP_Y1)]
    else:
        pts = [(x0, EP_Y0), (x1, EP_Y0), (x1, EP_Y1),
               (x0 + EP_CHX, EP_Y1), (x0, EP_Y1 - EP_CHY)]
    return (
        cq.Workplane("XY").workplane(offset=T - EP_D)
        .polyline(pts).close().extrude(EP_D + 1)
    )

part = part.cut(end_pocket(EPL_X0, EPL_X1, True))
part = part.cut(end_pocket(EPR_X0, EPR_X1, False))

# flange pocket: follows the concave front arc, clears the hole bosses
bx, by = FP_BOSS_C
p6x = ARC_CX + math.sqrt(FP_ARC_R ** 2 - (FP_Y_BOT - ARC_CY) ** 2)
p7x = 44.8
p7y = ARC_CY + math.sqrt(FP_ARC_R ** 2 - (p7x - ARC_CX) ** 2)
a45 = math.radians(135)
fpocket = (
    cq.Workplane("XY").workplane(offset=T - FP_D)
    .moveTo(FP_X0, FP_Y_TOP)
    .lineTo(FP_X1, FP_Y_TOP)
    .lineTo(FP_X1, FP_Y_STEP)
    .lineTo(bx, FP_Y_STEP)
    .threePointArc((bx + FP_BOSS_R * math.cos(a45), by + FP_BOSS_R * math.sin(a45)),
                   (bx - FP_BOSS_R, by))
    .lineTo(p6x, FP_Y_BOT)
    .threePointArc((ARC_CX, ARC_CY + FP_ARC_R), (p7x, p7y))
    .lineTo(FP_X0, -17.0)
    .close()
    .extrude(FP_D + 1)
)
part = part.cut(fpocket)

# flange holes
for (hx, hy) in F_HOLES:
    part = part.cut(
        cq.Workplane("XY").center(hx, hy).circle(F_HOLE_D / 2)
        .extrude(T + 1).translate((0, 0, -0.5))
    )

result = part
